import cadquery as cq

# =====================================================================
# Knurled thumb knob with rear hub (knurl left as a plain cylinder)
#   - flat grip face with a rounded rim
#   - knurled cylindrical head (plain cylinder here)
#   - rear skirt forming a recess around a projecting hub
#   - blind bore in the hub
# The knob axis lies in the YZ plane: the grip face normal points
# to -Y and is tilted TILT_DEG upward (+Z).
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
D_KNOB = 40.0          # knurled head diameter
T_HEAD = 11.0          # head thickness (grip face to rear rim)
FILLET_TOP = 2.4       # round on the grip face rim
RIM_WALL = 2.5         # wall thickness of the rear skirt
RECESS_DEPTH = 8.0     # depth of the rear recess inside the skirt
D_HUB = 25.8           # rear hub / boss diameter
L_HUB = 7.8            # hub protrusion beyond the rear rim
D_HOLE = 13.5          # blind bore in the hub
HOLE_DEPTH = L_HUB + RECESS_DEPTH   # bore ends at the recess floor level
TILT_DEG = 30.0        # grip-face normal tilted up from -Y by this angle
SEAM_TURN = 180.0      # spin about own axis (keeps B-rep seams on the far side)

R = D_KNOB / 2.0
R_IN = R - RIM_WALL
R_HUB = D_HUB / 2.0
R_HOLE = D_HOLE / 2.0

# ---------------- half cross-section in the XZ plane (x = radius) -------------
# local frame: grip face at z = T_HEAD, rear rim at z = 0, hub end at z = -L_HUB
profile = [
    (R_HOLE, -L_HUB),                       # bore mouth
    (R_HUB, -L_HUB),                        # hub end face
    (R_HUB, RECESS_DEPTH),                  # hub outer wall up to recess floor
    (R_IN, RECESS_DEPTH),                   # recess floor
    (R_IN, 0.0),                            # skirt inner wall
    (R, 0.0),                               # rear rim
    (R, T_HEAD),                            # knurled outer cylinder
    (0.0, T_HEAD),                          # grip face
    (0.0, -L_HUB + HOLE_DEPTH),             # axis down to bore bottom
    (R_HOLE, -L_HUB + HOLE_DEPTH),          # bore bottom
]

knob = (
    cq.Workplane("XZ")
    .polyline(profile)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)

# round the grip-face rim (outer circular edge at the top)
knob = knob.edges(
    cq.selectors.NearestToPointSelector((0.0, R, T_HEAD))
).fillet(FILLET_TOP)

# ---------------- orient: local +Z -> (0, -cos t, sin t) ----------------
knob = knob.rotate((0, 0, 0), (0, 0, 1), SEAM_TURN)
result = knob.rotate((0, 0, 0), (1, 0, 0), 90.0 - TILT_DEG)

VIEW = {"azimuth": 45, "elevation": 26}
